import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_X = 100.0      # base plate width  (X)
PLATE_Y = 130.0      # base plate depth  (Y)
PLATE_T = 10.6       # base plate thickness (Z)

BOX_X = 69.0         # bridge block width  (X)
BOX_Y = 55.0         # bridge block depth  (Y) - tunnel length
BOX_H = 36.3         # bridge block height above the plate

WALL_T = 10.5        # side-wall thickness of the bridge
TOP_T = 10.7         # top-slab thickness of the bridge

HOLE_D = 10.0        # plate mounting-hole diameter
HOLE_INSET = 20.8    # hole centre inset from the plate edges (X and Y)
TOP_HOLE_D = 10.0    # hole through the centre of the top slab

# derived
TUNNEL_W = BOX_X - 2 * WALL_T          # clear opening width (X)
TUNNEL_H = BOX_H - TOP_T               # clear opening height above plate top
Z_TOP = PLATE_T + BOX_H                # overall height

# ---------------- base plate ----------------
plate = cq.Workplane("XY").box(PLATE_X, PLATE_Y, PLATE_T, centered=(True, True, False))

# ---------------- bridge: inverted-U profile in XZ, extruded along Y ----------------
half_bx = BOX_X / 2
half_tw = TUNNEL_W / 2
bridge_profile = [
    (-half_bx, PLATE_T),
    (-half_tw, PLATE_T),
    (-half_tw, PLATE_T + TUNNEL_H),
    (half_tw, PLATE_T + TUNNEL_H),
    (half_tw, PLATE_T),
    (half_bx, PLATE_T),
    (half_bx, Z_TOP),
    (-half_bx, Z_TOP),
]
bridge = (
    cq.Workplane("XZ", origin=(0, BOX_Y / 2, 0))
    .polyline(bridge_profile)
    .close()
    .extrude(BOX_Y)            # XZ normal is -Y: extrudes from +BOX_Y/2 to -BOX_Y/2
)

body = plate.union(bridge)

# ---------------- rectangular window through the plate under the tunnel ----------------
window = (
    cq.Workplane("XY")
    .rect(TUNNEL_W, BOX_Y)
    .extrude(PLATE_T)
)
body = body.cut(window)

# ---------------- four corner mounting holes ----------------
hx = PLATE_X / 2 - HOLE_INSET
hy = PLATE_Y / 2 - HOLE_INSET
body = (
    body.faces("<Z").workplane(centerOption="CenterOfBoundBox")
    .pushPoints([(hx, hy), (-hx, hy), (hx, -hy), (-hx, -hy)])
    .hole(HOLE_D, PLATE_T)
)

# ---------------- hole through the top slab ----------------
body = (
    body.faces(">Z").workplane(centerOption="CenterOfBoundBox")
    .hole(TOP_HOLE_D, TOP_T)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
